import cadquery as cq

# Sheet-metal style tray/hood: open top and bottom, two side walls with a 45 deg
# sloped front edge, full-height back wall, low front lip joined to the side walls
# by vertical bends, four small bottom corner tabs.

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # outer width  (X)
D = 200.0          # outer depth  (Y)
H = 80.0           # outer height (Z)
T = 4.0            # sheet thickness
R_IN = 0.8         # inner bend radius of the two front vertical bends
R_OUT = R_IN + T

LIP_H = 19.0       # height of the low front lip
SLOPE_TOP_Y = -32.0  # Y where the 45 deg sloped edge reaches full height

# countersunk screw holes in both side walls (Y, Z)
CSK_HOLES = [(-87.9, 18.1), (-36.2, 69.9), (-10.0, 75.1), (59.8, 75.1)]
CSK_D = 8.0        # countersink diameter (90 deg)
HOLE_D = 3.9       # through hole

# large round hole in the left (-X) wall
BIG_HOLE_D = 20.0
BIG_HOLE_Y = -33.0
BIG_HOLE_Z = 16.4

# cut-out in the back wall (near +X side)
CUT_X0 = 18.4
CUT_X1 = W / 2 - T
CUT_Z0 = T
CUT_Z1 = 53.0
CUT_CH = 5.7

# small corner tabs on the bottom
TAB = 8.0
TAB_HOLE_D = 3.4
TAB_CSK_D = 4.2

# ---------------- body: closed tube with rounded front corners ----------------
outer = (cq.Workplane("XY").box(W, D, H, centered=(True, True, False))
         .edges("|Z and <Y").fillet(R_OUT))
inner = (cq.Workplane("XY").box(W - 2 * T, D - 2 * T, H + 2, centered=(True, True, False))
         .translate((0, 0, -1))
         .edges("|Z and <Y").fillet(R_IN))
body = outer.cut(inner)

# ---------------- top cut: V-notched low front + 45 deg slope ----------------
# the front lip top is bevelled at 45 deg (falling towards the back); it meets the
# 45 deg rising slope of the side walls in a V at (YV, ZV)
YV = (LIP_H - D / 2 - H + SLOPE_TOP_Y) / 2.0
ZV = LIP_H - (YV + D / 2)
top_cut = (cq.Workplane("YZ", origin=(-W, 0, 0))
           .polyline([(-D / 2 - 2, LIP_H + 2), (YV, ZV), (SLOPE_TOP_Y, H),
                      (SLOPE_TOP_Y, H + 5), (-D / 2 - 2, H + 5)]).close()
           .extrude(2 * W))
body = body.cut(top_cut)

# ---------------- corner tabs on the bottom ----------------
for sx in (1, -1):
    for sy in (1, -1):
        cx = sx * (W / 2 - T - TAB / 2)
        cy = sy * (D / 2 - T - TAB / 2)
        tab = (cq.Workplane("XY").box(TAB + 0.5, TAB + 0.5, T, centered=(True, True, False))
               .translate((cx + sx * 0.25, cy + sy * 0.25, 0)))
        body = body.union(tab)
        hole = cq.Solid.makeCylinder(TAB_HOLE_D / 2, 3 * T, cq.Vector(cx, cy, -T), cq.Vector(0, 0, 1))
        csk = cq.Solid.makeCone(TAB_CSK_D / 2 + 0.05, 0.0, TAB_CSK_D / 2 + 0.05,
                                cq.Vector(cx, cy, T + 0.05), cq.Vector(0, 0, -1))
        body = body.cut(cq.Workplane().add(hole.fuse(csk)))

# ---------------- countersunk holes in both side walls ----------------
def csk_tool(x_face, direction, y, z):
    e = 0.05
    rc = CSK_D / 2
    p = cq.Vector(x_face - direction * e, y, z)
    d = cq.Vector(direction, 0, 0)
    cone = cq.Solid.makeCone(rc + e, 0.0, rc + e, p, d)
    cyl = cq.Solid.makeCylinder(HOLE_D / 2, 3 * T, cq.Vector(x_face - direction * T, y, z), d)
    return cone.fuse(cyl)

for (y, z) in CSK_HOLES:
    body = body.cut(cq.Workplane().add(csk_tool(W / 2, -1, y, z)))
    body = body.cut(cq.Workplane().add(csk_tool(-W / 2, 1, y, z)))

# ---------------- large round hole in the -X wall ----------------
big = (cq.Workplane("YZ", origin=(-W / 2 - 1, 0, 0)).center(BIG_HOLE_Y, BIG_HOLE_Z)
       .circle(BIG_HOLE_D / 2).extrude(T + 2))
body = body.cut(big)

# ---------------- back wall cut-out ----------------
cut_pts = [(CUT_X0, CUT_Z0), (CUT_X1, CUT_Z0), (CUT_X1, CUT_Z1 - CUT_CH),
           (CUT_X1 - CUT_CH, CUT_Z1), (CUT_X0 + CUT_CH, CUT_Z1), (CUT_X0, CUT_Z1 - CUT_CH)]
back_cut = (cq.Workplane("XZ", origin=(0, D / 2 + 1, 0))
            .polyline(cut_pts).close().extrude(T + 2))
body = body.cut(back_cut)

result = body
